import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 300.0          # overall width  (X)
H = 233.0          # overall depth  (Y)
T = 5.6            # plate thickness (Z)
B = 5.0            # bar width of the frame
R_BACK = 7.5       # outer corner radius at the two back (+Y) corners
C_FRONT = 28.0     # outer corner cut at the two front (-Y) corners (leg length)
S_FRONT = 1.3      # outward bulge (sagitta) of the front corner cuts
C_IN_FRONT = 25.0  # inner 45deg chamfer at the front corners
C_IN_BACK = 25.0   # inner corner cut at the back corners (gusset edge)
S_IN_BACK = 1.0    # bulge of the gusset edge toward the outer corner

HOLE_D = 6.2       # corner mounting holes
HOLE_R_TOP = 1.5   # rounded (filleted) top edge of the holes
HOLE_OFF = 9.0     # hole centre offset from the outer edges

# hinge knuckles on the front edge
KN_R = 3.5         # knuckle radius
KN_FWD = 5.0       # knuckle axis in front of the front face
KN_UP = 4.9        # knuckle axis above the top face
PIN_D = 2.4        # pin hole diameter
KN_FOOT = 1.7      # tab foot (at z=0) sticks out this far in front of the front face
KNUCKLES = [(-104.0, 16.7), (90.4, 8.1), (116.0, 8.1)]  # (x centre, length)

# angled blind holes in the front face of the front bar (lean toward +X going inward)
SLOT_D = 3.5
SLOT_ANG = 67.0    # angle of the hole axis from the Y axis (deg)
SLOTS_X = [-77.0, 28.5]
SLOT_DEPTH = 7.0   # blind depth along the hole axis

# blind pocket on the inner face of the back bar
POCKET_X = 0.0
POCKET_L = 17.0
POCKET_H = 3.6
POCKET_Z = 0.2     # pocket centre offset above mid-thickness
POCKET_D = 2.0

r2 = math.sqrt(0.5)
x0, x1 = -W / 2, W / 2
y0, y1 = -H / 2, H / 2

# ---------------- outer outline ----------------
def bulge_mid(p, q, s, nx, ny):
    """midpoint of chord p-q pushed by s along (nx, ny)"""
    return ((p[0] + q[0]) / 2 + s * nx, (p[1] + q[1]) / 2 + s * ny)


fl_a, fl_b = (x0, y0 + C_FRONT), (x0 + C_FRONT, y0)       # front-left cut
fr_a, fr_b = (x1 - C_FRONT, y0), (x1, y0 + C_FRONT)       # front-right cut
k = R_BACK * (1 - r2)

outer = (
    cq.Workplane("XY")
    .moveTo(*fl_b)
    .lineTo(*fr_a)
    .threePointArc(bulge_mid(fr_a, fr_b, S_FRONT, r2, -r2), fr_b)
    .lineTo(x1, y1 - R_BACK)
    .threePointArc((x1 - k, y1 - k), (x1 - R_BACK, y1))
    .lineTo(x0 + R_BACK, y1)
    .threePointArc((x0 + k, y1 - k), (x0, y1 - R_BACK))
    .lineTo(*fl_a)
    .threePointArc(bulge_mid(fl_a, fl_b, S_FRONT, -r2, -r2), fl_b)
    .close()
    .extrude(T)
)

# ---------------- inner opening ----------------
ix0, ix1 = x0 + B, x1 - B
iy0, iy1 = y0 + B, y1 - B
br_a, br_b = (ix1, iy1 - C_IN_BACK), (ix1 - C_IN_BACK, iy1)   # back-right gusset edge
bl_a, bl_b = (ix0 + C_IN_BACK, iy1), (ix0, iy1 - C_IN_BACK)   # back-left gusset edge

inner = (
    cq.Workplane("XY")
    .moveTo(ix0 + C_IN_FRONT, iy0)
    .lineTo(ix1 - C_IN_FRONT, iy0)
    .lineTo(ix1, iy0 + C_IN_FRONT)
    .lineTo(*br_a)
    .threePointArc(bulge_mid(br_a, br_b, S_IN_BACK, r2, r2), br_b)
    .lineTo(*bl_a)
    .threePointArc(bulge_mid(bl_a, bl_b, S_IN_BACK, -r2, r2), bl_b)
    .lineTo(ix0, iy0 + C_IN_FRONT)
    .close()
    .extrude(T)
)

frame = outer.cut(inner)

# ---------------- corner holes with rounded top edge ----------------
hole_pts = [(x0 + HOLE_OFF, y1 - HOLE_OFF), (x1 - HOLE_OFF, y1 - HOLE_OFF)]
frame = (
    frame.faces(">Z").workplane(origin=(0, 0, T))
    .pushPoints(hole_pts)
    .hole(HOLE_D)
)
for (hx, hy) in hole_pts:
    e = HOLE_D / 2 + 0.5
    frame = (
        frame.edges(cq.selectors.BoxSelector((hx - e, hy - e, T - 0.1), (hx + e, hy + e, T + 0.1)))
        .fillet(HOLE_R_TOP)
    )

# ---------------- hinge knuckles ----------------
yc, zc = y0 - KN_FWD, T + KN_UP


def tangent(py, pz, side):
    dy, dz = py - yc, pz - zc
    d = math.hypot(dy, dz)
    a = math.atan2(dz, dy)
    ang = a + side * math.acos(KN_R / d)
    return (yc + KN_R * math.cos(ang), zc + KN_R * math.sin(ang)), ang


t_top, a_top = tangent(y0, T, +1)      # upper/back side of the teardrop
t_bot, a_bot = tangent(y0 - KN_FOOT, 0.0, -1)    # lower/front side of the teardrop
if a_bot < a_top:
    a_bot += 2 * math.pi
a_mid = (a_top + a_bot) / 2
mid = (yc + KN_R * math.cos(a_mid), zc + KN_R * math.sin(a_mid))

knuckles = None
for (kx, kl) in KNUCKLES:
    prof = (
        cq.Workplane("YZ", origin=(kx - kl / 2, 0, 0))
        .moveTo(y0 + 0.5, 0.0)
        .lineTo(y0 - KN_FOOT, 0.0)
        .lineTo(*t_bot)
        .threePointArc(mid, t_top)
        .lineTo(y0, T)
        .lineTo(y0 + 0.5, T)
        .close()
        .extrude(kl)
    )
    pin = (
        cq.Workplane("YZ", origin=(kx - kl / 2 - 1, 0, 0))
        .center(yc, zc)
        .circle(PIN_D / 2)
        .extrude(kl + 2)
    )
    kn = prof.cut(pin)
    knuckles = kn if knuckles is None else knuckles.union(kn)

frame = frame.union(knuckles)

# ---------------- angled blind holes in the front bar ----------------
for sx in SLOTS_X:
    a = math.radians(SLOT_ANG)
    d = cq.Vector(math.sin(a), math.cos(a), 0)
    start = cq.Vector(sx, y0, T / 2) - d * 10.0
    cyl = cq.Solid.makeCylinder(SLOT_D / 2, 10.0 + SLOT_DEPTH, start, d)
    frame = frame.cut(cq.Workplane("XY").add(cyl))

# ---------------- pocket on inner face of back bar ----------------
pocket = (
    cq.Workplane("XY")
    .box(POCKET_L, POCKET_D * 2, POCKET_H)
    .translate((POCKET_X, iy1, T / 2 + POCKET_Z))
)
frame = frame.cut(pocket)

result = frame
